import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 90.0          # outer length  (X)
W = 99.5          # outer width   (Y)
H = 29.0          # overall height (Z)
wall = 5.4        # side wall thickness
floor_t = 3.0     # bottom thickness

rim_t = 2.8       # outer rim thickness left standing above the lid ledge
ledge_depth = 3.0 # depth of the lid rabbet below the top face

hole_inset = 3.4  # lid screw hole centre inset from the outer faces
ear_r = 4.3       # radius of the corner "ears" around the lid screws
ear_blend = 12.0  # concave blend between ear and side wall
corner_r = 3.0    # corner radius of the base rectangle (hidden in ears)
pocket_r = 5.25   # radius of the rabbet pocket, centred on the inner cavity corner
screw_d = 3.0     # lid screw pilot hole
screw_depth = 8.0

inner_corner_r = 2.5
bottom_fillet = 3.5
top_fillet = 0.8

# corner posts under the ledge (hanging, 45 deg pointed bottom)
post_a = 4.5
post_top = 23.4
post_bot = 16.8
post_round = 0.5

# internal ribs
rib_t = 1.8
rib_h = 12.1                  # top of ribs (absolute Z)
xrib_y = 10.4                 # centre of the rib running along X
xrib_x0 = -30.3               # free end of the X rib
yrib_x = -3.1                 # centre of the rib running along Y
yrib_y1 = 40.4                # end of the Y rib (towards +Y)
pad_top = 5.3                 # raised floor of the +X/+Y compartment

# -X wall features
notch_y0, notch_y1 = 25.4, 38.8
notch_bottom = 18.0
port_y, port_z = 20.3, 10.6
port_d = 9.7
port_cb_d = 14.0
port_cb_depth = 1.5

# +X wall slot
slot_yc, slot_zc = 26.3, 10.8
slot_len, slot_h = 14.7, 6.0
slot_r = 1.5
slot_rec_margin = 1.5         # shallow recess around the slot on the inside
slot_rec_r = 3.0
slot_rec_depth = 1.4

# ---------------- derived ----------------
ix = L / 2 - wall
iy = W / 2 - wall
hx = L / 2 - hole_inset
hy = W / 2 - hole_inset
screw_pts = [(sx * hx, sy * hy) for sx in (-1, 1) for sy in (-1, 1)]

# ---------------- outer shell ----------------
outer_prof = (
    cq.Sketch()
    .rect(L, W)
    .vertices()
    .fillet(corner_r)
    .reset()
    .push(screw_pts)
    .circle(ear_r)
    .clean()
    .reset()
    .vertices()
    .fillet(ear_blend)
)
body = cq.Workplane("XY").placeSketch(outer_prof).extrude(H)
body = body.faces("<Z").edges().fillet(bottom_fillet)
body = body.faces(">Z").edges().fillet(top_fillet)

# main cavity
cav_prof = (
    cq.Sketch()
    .rect(2 * ix, 2 * iy)
    .vertices()
    .fillet(inner_corner_r)
)
cavity = (
    cq.Workplane("XY")
    .workplane(offset=floor_t)
    .placeSketch(cav_prof)
    .extrude(H)
)
body = body.cut(cavity)

# lid rabbet with round pockets in the corners (around the lid screws)
inner_corner_pts = [(sx * ix, sy * iy) for sx in (-1, 1) for sy in (-1, 1)]
rab_prof = (
    cq.Sketch()
    .rect(L - 2 * rim_t, W - 2 * rim_t)
    .push(inner_corner_pts)
    .circle(pocket_r)
    .clean()
)
rabbet = (
    cq.Workplane("XY")
    .workplane(offset=H - ledge_depth)
    .placeSketch(rab_prof)
    .extrude(ledge_depth + 1)
)
body = body.cut(rabbet)


# ---------------- corner posts ----------------
def corner_post():
    """Post in local frame: inner wall corner at the origin, post grows
    towards +X/+Y; underside is a 45 deg pyramid running into the corner."""
    a = post_a
    ov = 0.6  # overlap into the wall material
    z0 = post_bot - a - 1.0
    prof = [(-ov, post_top), (a, post_top), (a, post_bot),
            (0.0, post_bot - a), (-ov, post_bot - a)]
    # profile in XZ extruded along +Y
    px = (cq.Workplane("XZ").polyline(prof).close()
          .extrude(-(a + 2 * ov)).translate((0, -ov, 0)))
    # same profile in YZ extruded along +X
    py = (cq.Workplane("YZ").polyline(prof).close()
          .extrude(a + 2 * ov).translate((-ov, 0, 0)))
    # square section with the exposed vertical edge rounded
    sq = (cq.Workplane("XY").workplane(offset=z0)
          .center((a - ov) / 2, (a - ov) / 2)
          .rect(a + ov, a + ov).extrude(post_top - z0))
    sq = sq.edges("|Z").edges(">X and >Y").fillet(post_round)
    return px.intersect(py).intersect(sq)


post0 = corner_post()
for sx in (-1, 1):
    for sy in (-1, 1):
        p = post0
        if sx > 0:
            p = p.mirror("YZ")
        if sy > 0:
            p = p.mirror("XZ")
        p = p.translate((sx * ix, sy * iy, 0))
        body = body.union(p)

# ---------------- internal ribs ----------------
xrib = (cq.Workplane("XY").workplane(offset=floor_t - 0.1)
        .center((xrib_x0 + ix + 0.5) / 2, xrib_y)
        .rect(ix + 0.5 - xrib_x0, rib_t)
        .extrude(rib_h - floor_t + 0.1))
yrib = (cq.Workplane("XY").workplane(offset=floor_t - 0.1)
        .center(yrib_x, (xrib_y + yrib_y1) / 2)
        .rect(rib_t, yrib_y1 - xrib_y)
        .extrude(rib_h - floor_t + 0.1))
body = body.union(xrib).union(yrib)

# raised floor in the compartment bounded by the two ribs and the +X/+Y walls
pad_x0 = yrib_x - rib_t / 2
pad = (cq.Workplane("XY").workplane(offset=floor_t - 0.1)
       .center((pad_x0 + ix + 0.5) / 2, (xrib_y + iy + 0.5) / 2)
       .rect(ix + 0.5 - pad_x0, iy + 0.5 - xrib_y)
       .extrude(pad_top - floor_t + 0.1))
body = body.union(pad)

# ---------------- wall features ----------------
# notch in the top of the -X wall
notch = (cq.Workplane("XY").workplane(offset=notch_bottom)
         .center(-L / 2, (notch_y0 + notch_y1) / 2)
         .rect(2 * wall + 4, notch_y1 - notch_y0)
         .extrude(H))
body = body.cut(notch)

# round port through the -X wall with a counterbore on the inside
port = (cq.Workplane("YZ").workplane(offset=-L / 2 - 2)
        .center(port_y, port_z).circle(port_d / 2).extrude(wall + 4))
port_cb = (cq.Workplane("YZ").workplane(offset=-ix - port_cb_depth)
           .center(port_y, port_z).circle(port_cb_d / 2)
           .extrude(port_cb_depth + 2))
body = body.cut(port).cut(port_cb)

# rounded slot through the +X wall
slot = (cq.Workplane("YZ").workplane(offset=ix - 1)
        .center(slot_yc, slot_zc)
        .placeSketch(cq.Sketch().rect(slot_len, slot_h)
                     .vertices().fillet(slot_r))
        .extrude(wall + 4))
slot_rec = (cq.Workplane("YZ").workplane(offset=ix - 1)
            .center(slot_yc, slot_zc)
            .placeSketch(cq.Sketch()
                         .rect(slot_len + 2 * slot_rec_margin,
                               slot_h + 2 * slot_rec_margin)
                         .vertices().fillet(slot_rec_r))
            .extrude(1 + slot_rec_depth))
body = body.cut(slot).cut(slot_rec)

# lid screw pilot holes
for (px_, py_) in screw_pts:
    h = (cq.Workplane("XY").workplane(offset=H - ledge_depth - screw_depth)
         .center(px_, py_).circle(screw_d / 2).extrude(screw_depth + 1))
    body = body.cut(h)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
